import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Leg link actuator: motor/gearbox drum (axis = X) with a hollow truss arm
# rising along +Z to a clevis with a cross bolt.
# ---------------------------------------------------------------------------

# ---- motor drum -----------------------------------------------------------
R_BODY = 50.0          # main motor can radius
BODY_X0 = -35.0        # motor can -X end
BODY_X1 = 0.0          # motor can +X end
BAND_R = 46.0          # small step ring between can and output plate
BAND_X1 = 2.5

# gearbox end (-X)
GB_RING_R = 44.0       # gearbox ring (between the clip tabs)
GB_RING_X0 = -40.5
GB_TAB_N = 8
GB_TAB_A0 = 15.0
GB_TAB_X0 = -41.5
GB_TAB_R0 = 40.0
GB_TAB_R1 = 49.5
GB_TAB_W = 12.0
GB_TAB_SLOT_W = 4.0
GB_TAB_SLOT_D = 3.0
GB_HOUSING_R = 42.5
GB_HOUSING_X0 = -49.0
GB_HUB_R = 28.5
GB_HUB_X0 = -51.0
GB_BORE_R = 14.0
GB_HOLE_R = 24.0
GB_HOLE_D = 3.2

# ---- output ring plate (+X) ------------------------------------------------
RING_R = 47.5
RING_X0 = 2.5
RING_X1 = 16.0        # outer band face
RECESS_R = 30.0       # inner recess radius
RECESS_X = 11.5       # recess floor
HUB_R = 18.5
HUB_X1 = 14.5
BOLT_PCD_R = 23.0
BOLT_N = 8
CB_D = 8.0
CB_DEPTH = 1.8
BOLT_HOLE_D = 4.5
SCREW_HEAD_D = 6.4
STUB_HOLE = 3          # bolt-circle position carrying the output stub pin
SLOT_PCD_R = 39.0
SLOT_N = 12
SLOT_L = 11.5
SLOT_W = 5.8
SLOT_DEPTH = 3.0
SMALL_HOLE_D = 2.8

# ---- arm (profile in YZ) ---------------------------------------------------
ARM_Y0 = -4.0         # -Y edge of straight part
ARM_Y1 = 35.0         # +Y edge of straight part
TOP_Z = 232.0         # clevis bolt height
TOP_R = 13.0          # clevis ear end radius
LEFT_BEND_Z = 193.0   # -Y edge starts bending towards the top
RIGHT_BEND_Z = 157.0  # +Y edge starts bending towards the top
FIL_L = 35.0          # fillet arm -> ring, -Y side
FIL_R = 12.0          # fillet arm -> ring, +Y side
WALL = 4.0            # wall / plate thickness of the box truss

# arm in X (front view)
ARM_X0 = 10.5
ARM_X1 = 40.5
SLANT_Z0 = 12.0       # walls taper (tilted plane) down to the ring face
SLANT_Z1 = 57.0
FLARE_Z0 = 185.0      # side plates flare out into clevis ears
FLARE_Z1 = 205.0
EAR_T = 5.0
EAR_X0 = 5.5          # outer face of -X ear
EAR_X1 = 46.5         # outer face of +X ear
CLEVIS_FLOOR_Z = 203.0
PLATE_Z0 = 30.0      # lower end of the +X side plate
PLATE_SLOPE = 0.35   # dX/dZ of the bent lower part of the +X plate
PLATE_EDGE_Z0 = 47.0  # +X plate lower edge at ARM_Y0
PLATE_EDGE_Z1 = 38.0  # +X plate lower edge at ARM_Y1
GROOVE_R0 = 17.0
GROOVE_R1 = 37.0
GROOVE_W = 4.0

# clevis hardware
PIN_D = 8.0
HEAD_AF = 17.0
HEAD_H = 5.5
WASHER_D = 23.0
WASHER_T = 1.2
NUT_D = 12.5
NUT_H = 6.5
COLLAR_AF = 13.0
COLLAR_L = 6.0

# output pins
STUB_D = 6.5
STUB_X1 = 38.0

SEAM_ROT = -135.0

VIEW = {"azimuth": 45, "elevation": 26}

V = cq.Vector


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def yz(y, z, x=0.0):
    return V(x, y, z)


def xz(x, z, y=0.0):
    return V(x, y, z)


def prism_from_wire(wire, vec):
    face = cq.Face.makeFromWires(wire)
    return cq.Solid.extrudeLinear(face, vec)


def poly_wire(pts3):
    return cq.Wire.makePolygon(pts3, close=True)


def rounded_poly_wire(pts3, r):
    w = poly_wire(pts3)
    inner = w.offset2D(-r, "intersection")[0]
    return inner.offset2D(r, "arc")[0]


def cyl_x(r, x0, x1, y=0.0, z=0.0):
    # cylinder along X; its seam is turned to the lower back side (cosmetic)
    c = cq.Solid.makeCylinder(r, x1 - x0, V(0, 0, 0), V(1, 0, 0))
    return c.rotate(V(0, 0, 0), V(1, 0, 0), SEAM_ROT).translate(V(x0, y, z))


def hex_prism_x(af, x0, x1, y=0.0, z=0.0, rot=0.0):
    rc = af / math.sqrt(3.0)
    pts = []
    for i in range(6):
        a = math.radians(rot + 60 * i)
        pts.append(V(x0, y + rc * math.cos(a), z + rc * math.sin(a)))
    return prism_from_wire(poly_wire(pts), V(x1 - x0, 0, 0))


def tangent_point(px, pz, cx, cz, r, side):
    """tangent point on circle (cx,cz,r) from external point p; side=+1/-1"""
    dx, dz = px - cx, pz - cz
    L = math.hypot(dx, dz)
    phi = math.atan2(dz, dx)
    a = math.acos(r / L)
    ang = phi + side * a
    return cx + r * math.cos(ang), cz + r * math.sin(ang)


# ---------------------------------------------------------------------------
# arm outline (YZ), includes ring disc
# ---------------------------------------------------------------------------
def arm_outline_wire(x):
    # fillet on +Y side
    cyr = ARM_Y1 + FIL_R
    czr = math.sqrt((RING_R + FIL_R) ** 2 - cyr ** 2)
    tr_line = (ARM_Y1, czr)
    tr_ring = (RING_R * cyr / (RING_R + FIL_R), RING_R * czr / (RING_R + FIL_R))
    # fillet on -Y side
    cyl = ARM_Y0 - FIL_L
    czl = math.sqrt((RING_R + FIL_L) ** 2 - cyl ** 2)
    tl_line = (ARM_Y0, czl)
    tl_ring = (RING_R * cyl / (RING_R + FIL_L), RING_R * czl / (RING_R + FIL_L))

    # tangents to top circle
    tR = tangent_point(ARM_Y1, RIGHT_BEND_Z, 0.0, TOP_Z, TOP_R, +1)
    tL = tangent_point(ARM_Y0, LEFT_BEND_Z, 0.0, TOP_Z, TOP_R, -1)
    # make sure right tangent is the one on the +Y side
    if tR[0] < 0:
        tR = tangent_point(ARM_Y1, RIGHT_BEND_Z, 0.0, TOP_Z, TOP_R, -1)
    if tL[0] > 0:
        tL = tangent_point(ARM_Y0, LEFT_BEND_Z, 0.0, TOP_Z, TOP_R, +1)

    def fmid(c, r, p1, p2):
        mx = 0.5 * (p1[0] + p2[0]) - c[0]
        mz = 0.5 * (p1[1] + p2[1]) - c[1]
        L = math.hypot(mx, mz)
        return (c[0] + r * mx / L, c[1] + r * mz / L)

    mr = fmid((cyr, czr), FIL_R, tr_ring, tr_line)
    ml = fmid((cyl, czl), FIL_L, tl_line, tl_ring)

    P = lambda p: yz(p[0], p[1], x)
    edges = [
        cq.Edge.makeThreePointArc(P(tr_ring), P(mr), P(tr_line)),
        cq.Edge.makeLine(P(tr_line), P((ARM_Y1, RIGHT_BEND_Z))),
        cq.Edge.makeLine(P((ARM_Y1, RIGHT_BEND_Z)), P(tR)),
        cq.Edge.makeThreePointArc(P(tR), P((0.0, TOP_Z + TOP_R)), P(tL)),
        cq.Edge.makeLine(P(tL), P((ARM_Y0, LEFT_BEND_Z))),
        cq.Edge.makeLine(P((ARM_Y0, LEFT_BEND_Z)), P(tl_line)),
        cq.Edge.makeThreePointArc(P(tl_line), P(ml), P(tl_ring)),
        cq.Edge.makeThreePointArc(P(tl_ring), P((0.0, -RING_R)), P(tr_ring)),
    ]
    return cq.Wire.assembleEdges(edges)


# ---------------------------------------------------------------------------
# motor drum
# ---------------------------------------------------------------------------
body = cyl_x(R_BODY, BODY_X0, BODY_X1)
body = body.fuse(cyl_x(BAND_R, BODY_X1 - 0.01, BAND_X1 + 0.01))

# gearbox end: ring with slotted clip tabs
body = body.fuse(cyl_x(GB_RING_R, GB_RING_X0, BODY_X0 + 0.01))
for k in range(GB_TAB_N):
    a = GB_TAB_A0 + 360.0 * k / GB_TAB_N
    tab = cq.Solid.makeBox(BODY_X0 + 0.01 - GB_TAB_X0, GB_TAB_R1 - GB_TAB_R0, GB_TAB_W,
                           V(GB_TAB_X0, GB_TAB_R0, -GB_TAB_W / 2))
    slot = cq.Solid.makeBox(GB_TAB_SLOT_D + 0.5, GB_TAB_R1 - GB_TAB_R0 + 2, GB_TAB_SLOT_W,
                            V(GB_TAB_X0 - 0.5, GB_TAB_R0 - 1, -GB_TAB_SLOT_W / 2))
    tab = tab.cut(slot)
    body = body.fuse(tab.rotate(V(0, 0, 0), V(1, 0, 0), a))
body = body.fuse(cyl_x(GB_HOUSING_R, GB_HOUSING_X0, GB_RING_X0 + 0.01))
hub_gb = cyl_x(GB_HUB_R, GB_HUB_X0, GB_HOUSING_X0 + 0.01)
body = body.fuse(hub_gb)
body = body.cut(cyl_x(GB_BORE_R, GB_HUB_X0 - 1, GB_HUB_X0 + 6.0))
for i in range(8):
    a = math.radians(22.5 + 45 * i)
    body = body.cut(cyl_x(GB_HOLE_D / 2, GB_HUB_X0 - 1, GB_HUB_X0 + 4,
                          GB_HOLE_R * math.cos(a), GB_HOLE_R * math.sin(a)))

# ---------------------------------------------------------------------------
# arm + ring plate (two-view intersection)
# ---------------------------------------------------------------------------
X_LO, X_HI = -5.0, 60.0
outline = arm_outline_wire(X_LO)
prof = prism_from_wire(outline, V(X_HI - X_LO, 0, 0))          # full YZ profile
inner_outline = outline.offset2D(-WALL, "intersection")[0]
prof_in = prism_from_wire(inner_outline, V(X_HI - X_LO, 0, 0))
rim = prof.cut(prof_in)                                           # wall band


def xz_prism(pts):
    return prism_from_wire(poly_wire([xz(x, z, -80.0) for x, z in pts]), V(0, 160, 0))


# tilted plane: the arm's walls taper down onto the flat ring face
PA = V(RING_X1, 40.0, SLANT_Z0)
PB = V(RING_X1, -40.0, SLANT_Z0)
PC = V(ARM_X1, 15.0, SLANT_Z1)
PN = (PB - PA).cross(PC - PA).normalized()
if PN.x > 0:
    PN = PN * -1.0          # PN points towards -X (into the material)


def beyond_plane(offset):
    """solid on the far (+X) side of the tilted plane, limited to low Z"""
    origin = PA + PN * offset
    pl = cq.Plane(origin=origin, xDir=V(0, 1, 0).cross(PN).normalized(), normal=PN * -1.0)
    half = cq.Workplane(pl).rect(600, 600).extrude(300).val()
    return half.intersect(cq.Solid.makeBox(200, 400, 140, V(RING_X1, -200, -70)))


# side plates (front-view strips incl. the flare into the clevis ears)
def xz_prism_smooth(pts, smooth):
    """XZ profile through pts; segments whose start index is in `smooth`
    are S-shaped splines with vertical end tangents (smooth flare)."""
    edges = []
    n = len(pts)
    for i in range(n):
        p0 = xz(pts[i][0], pts[i][1], -80.0)
        p1 = xz(pts[(i + 1) % n][0], pts[(i + 1) % n][1], -80.0)
        if i in smooth:
            t = V(0, 0, 1) if p1.z > p0.z else V(0, 0, -1)
            edges.append(cq.Edge.makeSpline([p0, p1], tangents=[t, t]))
        else:
            edges.append(cq.Edge.makeLine(p0, p1))
    return prism_from_wire(cq.Wire.assembleEdges(edges), V(0, 160, 0))


plate_m = prof.intersect(xz_prism_smooth([
    (ARM_X0, -60.0), (ARM_X0 + WALL, -60.0), (ARM_X0 + WALL, FLARE_Z0),
    (EAR_X0 + EAR_T, FLARE_Z1), (EAR_X0 + EAR_T, 260.0), (EAR_X0, 260.0),
    (EAR_X0, FLARE_Z1), (ARM_X0, FLARE_Z0)], {2, 6}))
# +X plate: vertical, bent slightly inwards at its lower end
_ux, _uz = PLATE_SLOPE, 1.0
_L = math.hypot(_ux, _uz)
_nx, _nz = -_uz / _L * WALL, _ux / _L * WALL          # inward offset of the bend
_zin = SLANT_Z1 + _nz + (ARM_X1 - WALL - (ARM_X1 + _nx)) * _uz / _ux
_zlow = PLATE_Z0
_xlow = ARM_X1 - (SLANT_Z1 - _zlow) * PLATE_SLOPE
plate_p = prof.intersect(xz_prism_smooth([
    (_xlow + _nx, _zlow + _nz), (_xlow, _zlow), (ARM_X1, SLANT_Z1), (ARM_X1, FLARE_Z0),
    (EAR_X1, FLARE_Z1), (EAR_X1, 260.0), (EAR_X1 - EAR_T, 260.0),
    (EAR_X1 - EAR_T, FLARE_Z1), (ARM_X1 - WALL, FLARE_Z0), (ARM_X1 - WALL, _zin)], {3, 7}))
# lower edge of the +X plate runs just under the lowest truss window
pz0 = PLATE_EDGE_Z0
pz1 = PLATE_EDGE_Z1
plate_p = plate_p.cut(prism_from_wire(poly_wire([
    yz(-60.0, -60.0, X_LO), yz(60.0, -60.0, X_LO),
    yz(60.0, pz1 + (pz1 - pz0) / (ARM_Y1 - ARM_Y0) * (60.0 - ARM_Y1), X_LO),
    yz(-60.0, pz0 - (pz1 - pz0) / (ARM_Y1 - ARM_Y0) * (ARM_Y0 + 60.0), X_LO)]),
    V(X_HI - X_LO, 0, 0)))

# front/back walls (band along the outline), open above the clevis floor
walls = rim.intersect(xz_prism([
    (RING_X0, -60.0), (ARM_X1, -60.0), (ARM_X1, FLARE_Z0),
    (EAR_X1 - EAR_T, CLEVIS_FLOOR_Z), (EAR_X0 + EAR_T, CLEVIS_FLOOR_Z),
    (ARM_X0, FLARE_Z0), (ARM_X0, 58.0), (RING_X0 + 3.0, 47.0), (RING_X0, 44.0)]))
walls = walls.cut(beyond_plane(0.0))

ring = cyl_x(RING_R, RING_X0, RING_X1)
arm = ring.fuse(plate_m).fuse(plate_p).fuse(walls).clean()

# side-plate truss windows (YZ, through X)
SIDE_WINDOWS = [
    [(-0.5, 210.5), (13.7, 212.9), (16.2, 198.8), (3.2, 197.6)],
    [(2.5, 178.0), (20.5, 186.0), (28.5, 153.0)],
    [(0.5, 161.0), (30.0, 137.0), (0.5, 110.0)],
    [(1.5, 94.5), (30.5, 120.0), (30.5, 70.0)],
    [(3.0, 78.0), (29.0, 53.5), (28.0, 48.5), (0.0, 54.0)],
]
for w in SIDE_WINDOWS:
    wire = rounded_poly_wire([yz(y, z, X_LO) for y, z in w], 2.0)
    arm = arm.cut(prism_from_wire(wire, V(X_HI - X_LO, 0, 0)))

# front/back wall windows (XZ, through Y)
WX0, WX1 = 17.5, 34.0
FRONT_WINDOWS = [
    [(WX0 - 4.0, 193.5), (WX1 + 4.0, 193.5), (WX1, 165.5), (WX0, 165.5)],
    [(WX0, 153.5), (WX1, 153.5), (WX1, 111.5), (WX0, 111.5)],
    [(WX0, 103.5), (WX1, 103.5), (WX1, 62.5), (WX0, 62.5)],
    [(17.8, 55.5), (32.4, 55.5), (18.0, 30.0)],
]
for w in FRONT_WINDOWS:
    wire = rounded_poly_wire([xz(x, z, -80.0) for x, z in w], 2.0)
    arm = arm.cut(prism_from_wire(wire, V(0, 160, 0)))
# the bent part of the +Y wall is open up to the clevis
top_open = rounded_poly_wire([xz(x, z, 6.0) for x, z in [
    (WX0, 165.5), (WX1, 165.5), (WX1 + 4.0, 193.5), (WX1 + 4.0, 215.0),
    (WX0 - 4.0, 215.0), (WX0 - 4.0, 193.5)]], 2.0)
arm = arm.cut(prism_from_wire(top_open, V(0, 60, 0)))

# ---- ring plate features --------------------------------------------------
# inner recess
arm = arm.cut(cyl_x(RECESS_R, RECESS_X, X_HI))
arm = arm.fuse(cyl_x(HUB_R, RECESS_X - 0.01, HUB_X1))
# counterbored bolt circle
for i in range(BOLT_N - 1):
    a = math.radians(22.5 + 45 * i)
    y, z = BOLT_PCD_R * math.sin(a), BOLT_PCD_R * math.cos(a)
    arm = arm.cut(cyl_x(CB_D / 2, RECESS_X - CB_DEPTH, RECESS_X + 1, y, z))
    arm = arm.cut(cyl_x(BOLT_HOLE_D / 2, RING_X0 - 1, RECESS_X, y, z))
    if i != STUB_HOLE:
        # socket head cap screw seated in the counterbore
        head = cyl_x(SCREW_HEAD_D / 2, RECESS_X - CB_DEPTH - 0.3, RECESS_X - 0.3, y, z)
        head = head.cut(hex_prism_x(2.5, RECESS_X - 1.5, RECESS_X, y, z, 30))
        arm = arm.fuse(head)


# radial groove in place of the 8th bolt hole
ga = 22.5 + 45 * (BOLT_N - 1)
groove = (cq.Workplane("YZ", origin=(RECESS_X - 1.5, 0, 0))
          .transformed(rotate=(0, 0, 90 - ga))
          .center(0.5 * (GROOVE_R0 + GROOVE_R1), 0)
          .slot2D(GROOVE_R1 - GROOVE_R0, GROOVE_W)
          .extrude(RING_X1 + 0.5 - (RECESS_X - 1.5)))
arm = arm.cut(groove.val())


# obround pockets + small holes on the outer band
for i in range(SLOT_N):
    a = math.radians(15 + 30 * i)
    y, z = SLOT_PCD_R * math.sin(a), SLOT_PCD_R * math.cos(a)
    slot = (cq.Workplane("YZ", origin=(RING_X1 - SLOT_DEPTH, 0, 0))
            .center(y, z)
            .transformed(rotate=(0, 0, -math.degrees(a)))
            .slot2D(SLOT_L, SLOT_W)
            .extrude(SLOT_DEPTH + 0.5))
    arm = arm.cut(slot.val())
    a2 = math.radians(30 * i)
    y2, z2 = SLOT_PCD_R * math.sin(a2), SLOT_PCD_R * math.cos(a2)
    arm = arm.cut(cyl_x(SMALL_HOLE_D / 2, RING_X1 - 4.0, RING_X1 + 0.5, y2, z2))

part = body.fuse(arm)

# ---------------------------------------------------------------------------
# clevis hardware
# ---------------------------------------------------------------------------
ear_in0 = EAR_X0 + EAR_T
ear_in1 = EAR_X1 - EAR_T
hw = cyl_x(PIN_D / 2, EAR_X0 - NUT_H + 0.5, EAR_X1 + 1.0, 0, TOP_Z)
hw = hw.fuse(cyl_x(WASHER_D / 2, EAR_X1 - 0.01, EAR_X1 + WASHER_T, 0, TOP_Z))
hw = hw.fuse(hex_prism_x(HEAD_AF, EAR_X1 + WASHER_T - 0.01, EAR_X1 + WASHER_T + HEAD_H, 0, TOP_Z, 30))
hw = hw.fuse(cyl_x(NUT_D / 2, EAR_X0 - NUT_H, EAR_X0 + 0.01, 0, TOP_Z))   # round barrel nut
hw = hw.fuse(hex_prism_x(COLLAR_AF, ear_in0, ear_in0 + COLLAR_L, 0, TOP_Z, 30))
hw = hw.fuse(cyl_x(COLLAR_AF / 2, ear_in1 - COLLAR_L, ear_in1, 0, TOP_Z))
part = part.fuse(hw)

# output stub pin and small dowel on the ring face
a = math.radians(22.5 + 45 * STUB_HOLE)
sy, sz = BOLT_PCD_R * math.sin(a), BOLT_PCD_R * math.cos(a)
pin = cyl_x(STUB_D / 2, RECESS_X - CB_DEPTH - 1.0, 28.0, sy, sz)
pin = pin.fuse(cyl_x(2.2, 27.9, STUB_X1, sy, sz))
part = part.fuse(pin)
part = part.fuse(cyl_x(2.0, RING_X1 - 1, 27.0, -7.7, -33.6))

result = cq.Workplane("XY").add(part)
